import math

import cadquery as cq

# ---------------------------------------------------------------------------
# Five articulated "finger" plates (compliant segments) joined by a cross rod.
# Plates lie in the YZ plane, stacked along X.  Nose (fingertip) at -Y,
# lug with pin hole at +Y.
# ---------------------------------------------------------------------------

N_PLATES = 5
T = 12.9            # plate thickness (X)
PITCH = 21.8        # plate pitch (X)

ROD_Y, ROD_Z = 2.0, 14.4    # cross rod axis (hinge of the tip segment)
ROD_D = 8.0

HOLE_Y, HOLE_Z = 40.35, 49.9   # lug pin hole
HOLE_D = 6.0

GAP_W = 1.0          # width of the S shaped joint gap

# --- front (tip) segment -----------------------------------------------------
TOP_FLAT_Z = 40.5
TOP_FLAT_Y0 = -28.3                    # front edge of the flat top
# concave rising top shared by all tips (ends at the flat top)
FRONT_TOP = [(-55.5, 29.25), (-47.3, 29.6), (-40.3, 31.7), (-34.3, 35.2),
             (TOP_FLAT_Y0, TOP_FLAT_Z)]
SLOT1_Y0, SLOT1_Y1 = -17.1, -12.96     # vertical channel walls
SLOT1_ZB, SLOT1_ZT = 20.5, 26.42       # horizontal channel bottom / top
SLOT1_END = -2.34                      # horizontal channel end (+Y)
TAB_Z = 39.5

# nose variants: bottom of the tip segment (from the hinge notch) -> around
# the rounded nose -> top (continues into FRONT_TOP)
NOSES = {
    "A": [(-15.0, 0.95), (-30.0, 0.05), (-44.0, -0.45), (-51.0, -0.45), (-56.0, 0.3),
          (-60.2, 2.2), (-66.3, 6.6), (-69.7, 11.8), (-71.0, 18.7), (-70.2, 23.0),
          (-68.0, 26.5), (-63.7, 28.95)],
    "B": [(-15.0, 0.95), (-30.0, 0.1), (-42.0, -0.3), (-47.0, -0.1), (-52.4, 1.7),
          (-58.6, 5.2), (-62.6, 9.6), (-64.6, 14.6), (-64.9, 19.5), (-64.3, 24.0),
          (-62.4, 27.3), (-58.2, 29.25)],
    "C": [(-12.0, 1.2), (-24.0, 0.6), (-30.5, 0.4), (-35.6, 1.4), (-39.4, 3.1),
          (-43.3, 5.8), (-46.4, 9.2), (-49.9, 15.2), (-50.5, 22.2), (-49.2, 26.8)],
}
PLATE_NOSES = ["A", "A", "A", "B", "C"]

# --- middle segment -----------------------------------------------------------
MID_BUMP = [(-4.4, 36.9), (-3.4, 38.2), (-1.0, 37.6)]   # rounded lip at the joint
MID_TOP = [(6.7, 36.7), (14.5, 38.6), (20.6, 42.2), (25.6, 41.0), (27.6, 36.5)]
SLOT2_Y0, SLOT2_Y1 = 27.6, 33.3        # vertical channel walls
SLOT2_ZB, SLOT2_ZT = 21.84, 26.94
SLOT2_END = 19.02                      # horizontal channel end (-Y)

# --- lug / base segment -------------------------------------------------------
LUG_Y0, LUG_Y1 = 30.12, 50.58
LUG_TOP = 58.5
LUG_SIDE_Z = 48.0                       # straight lug sides end here
LUG_CORNER = (1.62, 2.34)               # dome shoulder point (from side, below top)
LUG_CORNER_ANG = 50.0                   # outline direction at that point (deg)
LUG_STEP_Z = 41.6                       # small step at the lug's front foot
BACK_Y = 60.48                          # back face of the base
SHOULDER = [(53.3, 38.25), (56.8, 35.8), (58.9, 32.6), (60.15, 28.4), (BACK_Y, 24.5)]
HOOK_TOP = 13.3
HOOK_TIP = (71.2, 11.9)
SLOT3_Y0, SLOT3_Y1 = 42.12, 46.26       # back slot vertical channel
SLOT3_ZB, SLOT3_ZT = 15.78, 21.66
SLOT3_END = 54.24


def lug_contour():
    """Points and tangents of the lug outline: straight sides blending into a
    flattened dome (one smooth curve, no tangent edges on the lug)."""
    y0, y1, zt = LUG_Y0, LUG_Y1, LUG_TOP
    yc = 0.5 * (y0 + y1)
    ca = math.cos(math.radians(LUG_CORNER_ANG))
    sa = math.sin(math.radians(LUG_CORNER_ANG))
    pts = [(y0, LUG_SIDE_Z), (y0 + LUG_CORNER[0], zt - LUG_CORNER[1]), (yc, zt),
           (y1 - LUG_CORNER[0], zt - LUG_CORNER[1]), (y1, LUG_SIDE_Z), (y1, 41.0)]
    tans = [(0.0, 1.0), (0.0, 1.0), (ca, sa), (1.0, 0.0), (ca, -sa), (0.0, -1.0),
            (0.0, -1.0)]
    return pts, tans


def plate_profile(nose_key):
    nose = NOSES[nose_key]
    y_top = nose[-1][0]
    top = [p for p in FRONT_TOP if p[0] > y_top + 3.0]

    r1 = (SLOT1_ZT - SLOT1_ZB) / 2.0
    r2 = (SLOT2_ZT - SLOT2_ZB) / 2.0
    r3 = (SLOT3_ZT - SLOT3_ZB) / 2.0

    w = cq.Workplane("YZ").moveTo(TOP_FLAT_Y0, TOP_FLAT_Z)
    w = w.lineTo(SLOT1_Y0 - 0.1, TOP_FLAT_Z)
    # L slot 1 (down, then towards +Y)
    w = w.lineTo(SLOT1_Y0 + 0.5, SLOT1_ZB + 1.8)
    w = w.threePointArc((SLOT1_Y0 + 1.1, SLOT1_ZB + 0.55), (SLOT1_Y0 + 2.4, SLOT1_ZB))
    w = w.lineTo(SLOT1_END - r1, SLOT1_ZB)
    w = w.threePointArc((SLOT1_END, SLOT1_ZB + r1), (SLOT1_END - r1, SLOT1_ZT))
    w = w.lineTo(SLOT1_Y1, SLOT1_ZT)
    w = w.lineTo(SLOT1_Y1, TAB_Z)
    # tab top, dip into the joint gap, middle segment top (one smooth curve)
    w = w.lineTo(-6.2, TAB_Z)
    w = w.threePointArc((-5.2, TAB_Z - 0.5), (-4.9, 37.6))
    w = w.lineTo(*MID_BUMP[0])
    w = w.threePointArc(MID_BUMP[1], MID_BUMP[2])
    w = w.spline(MID_TOP, tangents=[(0.97, -0.24), (0.0, -1.0)], scale=False,
                 includeCurrent=True)
    # L slot 2 (down, then towards -Y)
    w = w.lineTo(SLOT2_Y0, SLOT2_ZT)
    w = w.lineTo(SLOT2_END + r2, SLOT2_ZT)
    w = w.threePointArc((SLOT2_END, SLOT2_ZB + r2), (SLOT2_END + r2, SLOT2_ZB))
    w = w.lineTo(SLOT2_Y1 - 2.0, SLOT2_ZB)
    w = w.threePointArc((SLOT2_Y1 - 0.59, SLOT2_ZB + 0.59), (SLOT2_Y1, SLOT2_ZB + 2.0))
    w = w.lineTo(SLOT2_Y1, 40.2)
    w = w.threePointArc((SLOT2_Y1 - 1.2, LUG_STEP_Z - 0.3), (LUG_Y0, LUG_STEP_Z + 0.5))
    # lug: one smooth rounded contour
    lug_pts, lug_tans = lug_contour()
    w = w.spline(lug_pts, tangents=lug_tans, scale=False, includeCurrent=True)
    # shoulder down to the back face
    w = w.lineTo(LUG_Y1 - 0.2, 39.9)
    w = w.spline(SHOULDER, tangents=[(0.9, -0.44), (0.0, -1.0)], scale=False,
                 includeCurrent=True)
    w = w.lineTo(BACK_Y, HOOK_TOP + 2.0)
    w = w.threePointArc((BACK_Y + 0.59, HOOK_TOP + 0.59), (BACK_Y + 2.0, HOOK_TOP))
    # hook
    w = w.lineTo(70.1, HOOK_TOP)
    w = w.spline([HOOK_TIP, (70.1, 9.2), (66.7, 5.7), (61.1, 3.65), (54.2, 2.95),
                  (50.0, 3.3)], includeCurrent=True)
    w = w.threePointArc((SLOT3_Y1 + 0.9, 4.3), (SLOT3_Y1, 6.2))
    # back slot (up from the bottom, then towards +Y)
    w = w.lineTo(SLOT3_Y1, SLOT3_ZB)
    w = w.lineTo(SLOT3_END - r3, SLOT3_ZB)
    w = w.threePointArc((SLOT3_END, SLOT3_ZB + r3), (SLOT3_END - r3, SLOT3_ZT))
    w = w.lineTo(44.1, SLOT3_ZT)
    w = w.threePointArc((43.4, 22.8), (42.4, 22.3))
    w = w.lineTo(SLOT3_Y0, SLOT3_ZT - 0.4)
    w = w.lineTo(SLOT3_Y0, 5.0)
    w = w.threePointArc((SLOT3_Y0 - 0.6, 3.4), (SLOT3_Y0 - 2.1, 2.9))
    # bottom of the middle segment, notch under the hinge
    w = w.lineTo(10.4, 2.35)
    w = w.threePointArc((6.2, 4.1), (4.3, 7.2))
    w = w.threePointArc((3.6, 7.6), (3.05, 7.1))
    w = w.lineTo(3.1, 4.6)
    w = w.threePointArc((2.3, 2.45), (0.4, 1.75))
    # bottom of the tip segment, rounded nose and concave top: one smooth curve
    w = w.spline(nose + top, tangents=[(-0.999, -0.04), (0.64, 0.77)],
                 scale=False, includeCurrent=True)
    w = w.close()
    return w


def s_gap_cutter(x0):
    pts = [(-4.5, 38.5), (-4.1, 33.9), (-0.8, 31.6), (3.4, 29.9), (6.4, 27.3),
           (7.1, 23.9), (5.7, 20.3), (2.9, 17.7)]
    centre = cq.Workplane("YZ").spline(pts).val()
    h = GAP_W / 2.0
    left, right = [], []
    n = 12
    for k in range(n + 1):
        t = k / n
        p = centre.positionAt(t)
        d = centre.tangentAt(t)
        # in-plane normal (plane YZ): rotate tangent by 90 deg
        ny, nz = -d.z, d.y
        left.append((p.y + h * ny, p.z + h * nz))
        right.append((p.y - h * ny, p.z - h * nz))
    pe, de = centre.positionAt(1.0), centre.tangentAt(1.0)
    ps, ds = centre.positionAt(0.0), centre.tangentAt(0.0)
    w = (cq.Workplane("YZ", origin=(x0 - 1.0, 0, 0))
         .moveTo(*left[0]).spline(left[1:], includeCurrent=True)
         .threePointArc((pe.y + h * de.y, pe.z + h * de.z), right[-1])
         .spline(list(reversed(right[:-1])), includeCurrent=True)
         .threePointArc((ps.y - h * ds.y, ps.z - h * ds.z), left[0])
         .close())
    return w.extrude(T + 2.0)


plates = None
for i, key in enumerate(PLATE_NOSES):
    x0 = i * PITCH
    prof = plate_profile(key)
    solid = prof.extrude(T).translate((x0, 0, 0))
    # pin hole through the lug
    hole = (cq.Workplane("YZ", origin=(x0 - 1.0, 0, 0))
            .center(HOLE_Y, HOLE_Z).circle(HOLE_D / 2.0).extrude(T + 2.0))
    solid = solid.cut(hole).cut(s_gap_cutter(x0))
    plates = solid if plates is None else plates.union(solid)

# cross rod through the tip hinges
rod = (cq.Workplane("YZ", origin=(0, 0, 0)).center(ROD_Y, ROD_Z)
       .circle(ROD_D / 2.0).extrude((N_PLATES - 1) * PITCH + T))
result = plates.union(rod)
